import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 85.0          # outer length along X
W = 98.2          # outer width along Y
H = 28.8          # outer height along Z (open top)
WALL = 2.0        # wall thickness
FLOOR = 2.0       # floor thickness
R_VERT = 2.0      # outer vertical edge radius
R_BOT = 2.0       # bottom edge fillet radius

# mounting posts (flush with the rim)
POST_D = 8.2
POST_HOLE_D = 1.6
POST_HOLE_DEPTH = 20.0
POST_X = -5.1
POST_Y = 36.6
POST_TOP = H

# front wall (-Y): double-D round hole
RH_X = 5.6
RH_Z = 7.5
RH_D = 8.0
RH_FLAT = 6.4     # distance between the two flats

# front wall (-Y): micro-USB shaped cut
MU_X = 27.4
MU_Z = 6.0
MU_W = 10.7
MU_H = 4.1
MU_CH = 1.55      # bottom corner chamfer
MU_R = 0.4        # top corner radius

# right wall (+X): rounded slot
OB_Y = 9.8
OB_Z = 6.5
OB_L = 13.4
OB_H = 6.0
OB_R = 2.6

# back wall (+Y): rectangular opening
RO_X0 = 3.3
RO_X1 = 20.7
RO_Z0 = 4.1
RO_Z1 = 15.4

CUT_T = 3 * WALL  # depth of through-cut tools (centred on the wall)

# ---------------- body ----------------
outer = (
    cq.Workplane("XY")
    .rect(L, W)
    .extrude(H)
    .edges("|Z")
    .fillet(R_VERT)
    .faces("<Z")
    .edges()
    .fillet(R_BOT)
)
cavity = (
    cq.Workplane("XY")
    .workplane(offset=FLOOR)
    .rect(L - 2 * WALL, W - 2 * WALL)
    .extrude(H)
)
body = outer.cut(cavity)

# ---------------- mounting posts ----------------
post_pts = [(POST_X, POST_Y), (POST_X, -POST_Y)]
posts = (
    cq.Workplane("XY")
    .workplane(offset=FLOOR - 0.01)
    .pushPoints(post_pts)
    .circle(POST_D / 2)
    .extrude(POST_TOP - FLOOR + 0.01)
)
body = body.union(posts)
post_holes = (
    cq.Workplane("XY")
    .workplane(offset=POST_TOP - POST_HOLE_DEPTH)
    .pushPoints(post_pts)
    .circle(POST_HOLE_D / 2)
    .extrude(POST_HOLE_DEPTH + 1)
)
body = body.cut(post_holes)

# ---------------- front wall (-Y) cut-outs ----------------
front_y = -W / 2 + WALL / 2

# double-D hole: circle trimmed by two horizontal flats
dd_sketch = (
    cq.Sketch()
    .circle(RH_D / 2)
    .rect(RH_D + 1, RH_FLAT, mode="i")
)
rh = (
    cq.Workplane("XZ", origin=(RH_X, front_y, RH_Z))
    .placeSketch(dd_sketch)
    .extrude(CUT_T / 2, both=True)
)
body = body.cut(rh)

# micro-USB outline: flat top with small radii, chamfered bottom corners
hw = MU_W / 2
hh = MU_H / 2
mu_pts = [
    (-hw, hh),
    (hw, hh),
    (hw, -hh + MU_CH),
    (hw - MU_CH, -hh),
    (-hw + MU_CH, -hh),
    (-hw, -hh + MU_CH),
]
mu_sketch = cq.Sketch().polygon(mu_pts).vertices(">Y").fillet(MU_R)
mu = (
    cq.Workplane("XZ", origin=(MU_X, front_y, MU_Z))
    .placeSketch(mu_sketch)
    .extrude(CUT_T / 2, both=True)
)
body = body.cut(mu)

# ---------------- right wall (+X) slot ----------------
ob_sketch = cq.Sketch().rect(OB_L, OB_H).vertices().fillet(OB_R)
ob = (
    cq.Workplane("YZ", origin=(L / 2 - WALL / 2, OB_Y, OB_Z))
    .placeSketch(ob_sketch)
    .extrude(CUT_T / 2, both=True)
)
body = body.cut(ob)

# ---------------- back wall (+Y) rectangular opening ----------------
ro = (
    cq.Workplane(
        "XZ",
        origin=((RO_X0 + RO_X1) / 2, W / 2 - WALL / 2, (RO_Z0 + RO_Z1) / 2),
    )
    .rect(RO_X1 - RO_X0, RO_Z1 - RO_Z0)
    .extrude(CUT_T / 2, both=True)
)
body = body.cut(ro)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
